import cadquery as cq

# Display bezel (16x2-style LCD front frame): an open-fronted shallow box whose
# thick back plate carries the display window, two blind side notches, four
# counter-bored display screws and four counter-bored corner screws.
# Open side faces -Y, closed (rounded) back faces +Y.

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # outer width  (X)
H = 72.8           # outer height (Z)
D = 18.4           # overall depth (Y)
WALL = 4.5         # side wall thickness
PLATE = 7.4        # back plate thickness (closed side, +Y)
R_CORNER = 2.5     # radius of the 4 outer edges running along Y
R_BACK = 4.0       # fillet around the back face outline

WIN_W = 65.3       # display window width
WIN_H = 25.0       # display window height
WIN_Z = 1.0        # window centre height offset (above part centre)

NOTCH_W = 4.3      # side notch width (X) beyond the window edge
NOTCH_H = 14.7     # side notch height (Z)
NOTCH_Z = 0.5      # notch centre height
NOTCH_DEPTH = 3.6  # notch depth into the plate from its inside face

LCD_HOLE_DX = 72.6     # display mounting hole spacing (X)
LCD_HOLE_DZ = 22.9     # display mounting hole spacing (Z)
LCD_HOLE_D = 2.6
LCD_CB_D = 5.5         # counterbore on the back face
LCD_CB_DEPTH = 4.0

CORNER_INSET = 2.9     # corner hole centre from the outer faces
CORNER_HOLE_D = 2.6
CORNER_CB_D = 5.5      # counterbore on the back face
CORNER_CB_DEPTH = 3.0

# ---------------- derived ----------------
cav_depth = D - PLATE
plate_front_y = -D / 2 + cav_depth      # inside face of the back plate

lcd_pts = [
    (sx * LCD_HOLE_DX / 2, WIN_Z + sz * LCD_HOLE_DZ / 2)
    for sx in (-1, 1)
    for sz in (-1, 1)
]
corner_pts = [
    (sx * (W / 2 - CORNER_INSET), sz * (H / 2 - CORNER_INSET))
    for sx in (-1, 1)
    for sz in (-1, 1)
]


def back_wp():
    """Workplane just behind the back face; positive extrude goes toward -Y."""
    return cq.Workplane("XZ", origin=(0, D / 2 + 1, 0))


# ---------------- outer shell ----------------
body = cq.Workplane("XY").box(W, D, H)
body = body.edges("|Y").fillet(R_CORNER)
body = body.faces(">Y").edges().fillet(R_BACK)

# cavity from the open front (-Y)
cavity = (
    cq.Workplane("XZ", origin=(0, -D / 2, 0))
    .rect(W - 2 * WALL, H - 2 * WALL)
    .extrude(-cav_depth)
)
body = body.cut(cavity)

# display window through the plate
window = back_wp().center(0, WIN_Z).rect(WIN_W, WIN_H).extrude(D + 2)
body = body.cut(window)

# blind side notches, cut from the inside face of the plate, open to the window
notch_span = NOTCH_W + 1.0          # 1 mm overlap into the (already empty) window
notch_cx = WIN_W / 2 + NOTCH_W - notch_span / 2
notches = (
    cq.Workplane("XZ", origin=(0, plate_front_y, 0))
    .pushPoints([(-notch_cx, NOTCH_Z), (notch_cx, NOTCH_Z)])
    .rect(notch_span, NOTCH_H)
    .extrude(-NOTCH_DEPTH)
)
body = body.cut(notches)

# display mounting holes, counterbored from the back
body = body.cut(back_wp().pushPoints(lcd_pts).circle(LCD_HOLE_D / 2).extrude(D + 2))
body = body.cut(back_wp().pushPoints(lcd_pts).circle(LCD_CB_D / 2).extrude(LCD_CB_DEPTH + 1))

# corner holes through the walls, counterbored from the back
body = body.cut(back_wp().pushPoints(corner_pts).circle(CORNER_HOLE_D / 2).extrude(D + 2))
body = body.cut(back_wp().pushPoints(corner_pts).circle(CORNER_CB_D / 2).extrude(CORNER_CB_DEPTH + 1))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
